import cadquery as cq
from OCP.BRepBuilderAPI import BRepBuilderAPI_NurbsConvert

# ---------------- driving dimensions (mm) ----------------
PLATE_W = 80.0          # square base plate side
PLATE_T = 1.25          # base plate thickness
PLATE_R = 4.0           # plate corner radius (plan view)

SPIKE_PITCH = 30.0      # 3 x 3 grid pitch
SPIKE_N = 3
SPIKE_H = 80.35         # spike height above plate top
SPIKE_BASE = 4.0        # square base side
SPIKE_TIP = 1.15        # square tip side

TEXT_H = 0.4            # embossed lettering height above the plate
FONT = "DejaVu Sans"    # rounded sans stand-in for the original lettering
# lettering is laid out glyph by glyph: (glyph, x-centre, overall width)
# "Orca" on the rear half of the plate
TEXT1 = [("O", -18.5, 17.0), ("r", -2.75, 9.5), ("c", 9.0, 10.6),
         ("\u0251", 21.4, 11.6)]          # single-storey a
TEXT1_SIZE = 25.0
TEXT1_BASE_Y = 10.5     # baseline y
TEXT1_GROW = 0.0        # stroke thickening (2D outline offset)
TEXT1_FIT = 1.0         # glyph width factor
# "Stringhell" (bolder, smaller, in front of the middle spike row)
TEXT2 = [("S", -26.4, 8.8), ("t", -18.7, 6.2), ("r", -12.1, 5.8),
         ("i", -6.9, 2.4), ("n", -1.7, 6.2), ("g", 5.25, 6.5),
         ("h", 12.95, 6.5), ("e", 20.65, 6.7), ("l", 26.2, 1.9),
         ("l", 29.9, 1.9)]
TEXT2_SIZE = 12.8
TEXT2_BASE_Y = -19.75
TEXT2_GROW = 0.35
TEXT2_FIT = 0.92        # glyph width factor (DejaVu outlines are boxier)

# ---------------- base plate ----------------
plate = (
    cq.Workplane("XY")
    .rect(PLATE_W, PLATE_W)
    .extrude(PLATE_T)
    .edges("|Z")
    .fillet(PLATE_R)
)

# ---------------- tapered square spikes ----------------
spike = (
    cq.Workplane("XY")
    .rect(SPIKE_BASE, SPIKE_BASE)
    .workplane(offset=SPIKE_H)
    .rect(SPIKE_TIP, SPIKE_TIP)
    .loft(combine=True)
)
spike_solid = spike.val()

result = plate
off = (SPIKE_N - 1) / 2.0
for i in range(SPIKE_N):
    for j in range(SPIKE_N):
        x = (i - off) * SPIKE_PITCH
        y = (j - off) * SPIKE_PITCH
        s = spike_solid.moved(cq.Location(cq.Vector(x, y, PLATE_T)))
        result = result.union(cq.Workplane("XY").add(s))

# ---------------- embossed lettering ----------------
def _nurbs_wire(w):
    """Re-express a (possibly offset-curve) wire with plain B-spline edges."""
    return cq.Wire(BRepBuilderAPI_NurbsConvert(w.wrapped, True).Shape())


def glyph_solid(ch, size, grow, width):
    """One raised glyph (baseline at y=0), stretched in X to 'width' overall;
    'grow' thickens the strokes by a 2D offset of the glyph outlines to mimic
    a heavier font weight."""
    base = (
        cq.Workplane("XY")
        .text(ch, size, TEXT_H, font=FONT, kind="regular", halign="left", valign="bottom")
        .val()
    )
    kx = (width - 2.0 * grow) / base.BoundingBox().xlen
    if abs(kx - 1.0) < 1e-3 and grow <= 0:
        return base
    stretch = cq.Matrix([[kx, 0, 0, 0], [0, 1, 0, 0], [0, 0, 1, 0]])

    def shape_wire(w, d):
        w = cq.Wire(w.transformGeometry(stretch).wrapped)
        if d != 0:
            w = w.offset2D(d, "arc")[0]
        return _nurbs_wire(w)

    try:
        solids = []
        for f in base.Faces():
            if f.normalAt().z > -0.5:
                continue  # keep only the glyph bottom faces
            outer = shape_wire(f.outerWire(), grow)
            inner = [shape_wire(w, -grow) for w in f.innerWires()]
            nf = cq.Face.makeFromWires(outer, inner)
            solids.append(cq.Solid.extrudeLinear(nf, cq.Vector(0, 0, TEXT_H)))
        grown = solids[0]
        for sd in solids[1:]:
            grown = grown.fuse(sd)
        return grown.clean()
    except Exception:
        return base


def emboss(wp, letters, size, base_y, grow, fit):
    for ch, cx, width in letters:
        try:
            g = glyph_solid(ch, size, grow, width * fit)
            bb = g.BoundingBox()
            dx = cx - 0.5 * (bb.xmin + bb.xmax)
            g = g.moved(cq.Location(cq.Vector(dx, base_y, PLATE_T)))
            wp = wp.union(cq.Workplane("XY").add(g))
        except Exception:
            pass
    return wp


result = emboss(result, TEXT1, TEXT1_SIZE, TEXT1_BASE_Y, TEXT1_GROW, TEXT1_FIT)
result = emboss(result, TEXT2, TEXT2_SIZE, TEXT2_BASE_Y, TEXT2_GROW, TEXT2_FIT)

VIEW = {"azimuth": 45, "elevation": 26}
